import cadquery as cq

# Open electronics tray (bottom shell of an enclosure) with a belt clip on the
# underside: thin walls, a slightly thicker lower tier inside, corner blocks,
# a back shelf, a walled pocket in the back-right corner, low ribs, locating
# pins, a long slot in the back wall and a notch in the right wall.

# ---------------- driving dimensions (mm) ----------------
L = 100.0           # outer length (X)
W = 73.0            # outer width (Y)
H = 21.75           # outer height (Z)
T = 1.4             # wall thickness
TF = 1.4            # floor thickness
R_OUT = 1.5         # outer vertical corner radius
R_IN = 1.4          # inner vertical corner radius
R_BOT = 1.4         # bottom outer edge fillet

Z_TIER = 5.7        # top of the lower (thicker) tier of the inner walls
E_TIER = 0.3        # inset of the lower tier (small step along the walls)
R_SHELF_COVE = 1.5  # cove where the back shelf meets the back wall
C_CORNER_BL = 4.0   # chamfer legs of the back-left corner block
C_CORNER_FL = 4.4   # front-left corner block
C_CORNER_FR = 2.0   # front-right corner block (inside the L rib)

# back shelf and back-right block (outline of the raised lower tier)
SHELF_Y = 31.0      # front face of the back shelf
SHELF_X = -17.6     # left end of the shelf front (45 deg chamfer back to wall)
BLOCK_X = 38.25     # left face of the back-right block
BLOCK_Y = 12.3      # front face of the back-right block
BLOCK_CH_TL = 4.25  # chamfer shelf -> block
BLOCK_CH_BL = 2.0   # chamfer at the block's front-left corner
BLOCK_CH_BR = 1.5   # chamfer where the block meets the right wall
# pocket inside the back-right block
POCKET_X0, POCKET_X1 = 40.0, 45.6
POCKET_Y0, POCKET_Y1 = 13.75, 32.3
POCKET_CH = 3.7

Z_RIB = 4.0         # top of the low ribs
RIB_FL_X1 = -2.8    # right end of the front-left rib
RIB_FR_X0 = 22.1    # left end of the front-right L rib
RIB_FRONT_Y = -33.0 # back face of the front ribs
RIB_SIDE_X = 46.6   # inner face of the L rib leg along the right wall
RIB_SIDE_Y = -30.0  # end of the L rib leg
R_RIB = 0.8         # rounding of the L rib corners
RIB_BACK_X0, RIB_BACK_X1 = 5.0, 36.0
RIB_BACK_Y = 28.9   # front face of the low rib in front of the back shelf

PIN_H = 2.7
PIN_BIG_D = 6.1
PIN_BIG = (6.1, -3.5)
# (x, y, diameter) of the small locating pins on the floor
PINS = [(-39.7, 23.6, 3.3), (-39.6, -5.75, 4.0)]

# slot in back wall
SLOT_X0, SLOT_X1 = -21.3, 35.6
SLOT_Z0, SLOT_Z1 = 9.7, 13.5
SLOT_R = 0.8

# notch in right wall
NOTCH_W = 12.25
NOTCH_Z = 13.5
NOTCH_R = 1.0

# belt clip under the floor
CLIP_Y_FRONT = -27.4     # where the clip leaves the box bottom
CLIP_Y_BACKFACE = -15.3  # back face of the solid ramp (start of the gap)
CLIP_Y_FLAT = -12.0      # where the curved ramp becomes the flat tongue bottom
CLIP_HW_TOP = 24.6       # half width at the attachment
CLIP_HW = 16.2           # half width of the tongue
CLIP_DEPTH = 4.6         # how far the clip hangs under the box
CLIP_GAP = 1.7           # gap between box bottom and tongue
CLIP_Y_TIP = 32.3        # tongue tip
CLIP_Y_SLOPE = 23.5      # start of the rounded-down tip
BUMP_Y0, BUMP_Y1, BUMP_H = 5.5, 12.5, 0.5   # detent bump on the tongue
CLIP_CORNER_Z = 2.3      # height of the rounded lower corners of the flares

xi = L / 2 - T           # inner wall x
yi = W / 2 - T           # inner wall y
xl = xi - E_TIER         # lower tier x
yl = yi - E_TIER         # lower tier y


def block(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center((x0 + x1) / 2, (y0 + y1) / 2)
            .rect(abs(x1 - x0), abs(y1 - y0)).extrude(z1 - z0))


# ---------------- outer shell ----------------
outer = (cq.Workplane("XY").rect(L, W).extrude(H)
         .edges("|Z").fillet(R_OUT)
         .faces("<Z").edges().fillet(R_BOT))

# upper cavity (full inner outline)
cav_up = (cq.Workplane("XY").workplane(offset=Z_TIER)
          .rect(2 * xi, 2 * yi).extrude(H)
          .edges("|Z").fillet(R_IN))

# lower cavity: polygon with corner blocks, back shelf and back-right block
lower_pts = [
    (-xl, -yl + C_CORNER_FL), (-xl + C_CORNER_FL, -yl),      # front-left block
    (xl - C_CORNER_FR, -yl), (xl, -yl + C_CORNER_FR),        # front-right block
    (xl, BLOCK_Y - BLOCK_CH_BR),                             # back-right block
    (xl - BLOCK_CH_BR, BLOCK_Y),
    (BLOCK_X + BLOCK_CH_BL, BLOCK_Y),
    (BLOCK_X, BLOCK_Y + BLOCK_CH_BL),
    (BLOCK_X, SHELF_Y - BLOCK_CH_TL),
    (BLOCK_X - BLOCK_CH_TL, SHELF_Y),
    (SHELF_X, SHELF_Y), (SHELF_X - (yl - SHELF_Y), yl),      # back shelf
    (-xl + C_CORNER_BL, yl), (-xl, yl - C_CORNER_BL),        # back-left block
]
cav_lo = (cq.Workplane("XY").workplane(offset=TF)
          .polyline(lower_pts).close().extrude(Z_TIER - TF))

body = outer.cut(cav_up).cut(cav_lo)

# cove where the back shelf meets the back wall
rc = R_SHELF_COVE
shelf_x0 = SHELF_X - (yl - SHELF_Y)
shelf_cove = (cq.Workplane("YZ", origin=(shelf_x0, 0, 0))
              .moveTo(yi - rc, Z_TIER)
              .lineTo(yi + 0.2, Z_TIER)
              .lineTo(yi + 0.2, Z_TIER + rc)
              .lineTo(yi, Z_TIER + rc)
              .radiusArc((yi - rc, Z_TIER), -rc)
              .close()
              .extrude(xi - shelf_x0))
shelf_cove = shelf_cove.cut(cq.Workplane("XY").workplane(offset=Z_TIER - 1)
                            .polyline(lower_pts).close().extrude(rc + 2))
body = body.union(shelf_cove)

# ---------------- low ribs on the floor ----------------
ribs = [
    block(-xl - 0.2, RIB_FL_X1, -yl - 0.2, RIB_FRONT_Y, TF - 0.1, Z_RIB),
    block(RIB_BACK_X0, RIB_BACK_X1, RIB_BACK_Y, SHELF_Y + 0.2, TF - 0.1, Z_RIB),
]
# L-shaped rib in the front-right corner (along front wall, up the right wall)
rr = R_RIB
l_rib = (cq.Workplane("XY").workplane(offset=TF - 0.1)
         .moveTo(RIB_FR_X0, -yl - 0.2)
         .lineTo(xl + 0.2, -yl - 0.2)
         .lineTo(xl + 0.2, RIB_SIDE_Y)
         .lineTo(RIB_SIDE_X + rr, RIB_SIDE_Y)
         .radiusArc((RIB_SIDE_X, RIB_SIDE_Y - rr), -rr)
         .lineTo(RIB_SIDE_X, RIB_FRONT_Y + rr)
         .radiusArc((RIB_SIDE_X - rr, RIB_FRONT_Y), rr)
         .lineTo(RIB_FR_X0, RIB_FRONT_Y)
         .close()
         .extrude(Z_RIB - TF + 0.1))
ribs.append(l_rib)
for r in ribs:
    body = body.union(r)

# pocket in the back-right block
pocket_pts = [
    (POCKET_X0 - POCKET_CH, POCKET_Y1), (POCKET_X1, POCKET_Y1),
    (POCKET_X1, POCKET_Y0), (POCKET_X0, POCKET_Y0),
    (POCKET_X0, POCKET_Y1 - POCKET_CH - 0.9), (POCKET_X0 - POCKET_CH, POCKET_Y1 - 0.7),
]
pocket = (cq.Workplane("XY").workplane(offset=Z_RIB)
          .polyline(pocket_pts).close().extrude(Z_TIER - Z_RIB + 0.5))
body = body.cut(pocket)

# ---------------- pins ----------------
for (px, py, pd) in PINS:
    body = body.union(cq.Workplane("XY").workplane(offset=TF - 0.1)
                      .center(px, py).circle(pd / 2).extrude(PIN_H + 0.1))
body = body.union(cq.Workplane("XY").workplane(offset=TF - 0.1)
                  .center(*PIN_BIG).circle(PIN_BIG_D / 2).extrude(PIN_H + 0.1))

# ---------------- slot in back wall ----------------
slot = (cq.Workplane("XZ", origin=(0, W / 2 + 1.0, 0))
        .center((SLOT_X0 + SLOT_X1) / 2, (SLOT_Z0 + SLOT_Z1) / 2)
        .rect(SLOT_X1 - SLOT_X0, SLOT_Z1 - SLOT_Z0).extrude(T + 2.0)
        .edges("|Y").fillet(SLOT_R))
body = body.cut(slot)

# ---------------- notch in right wall ----------------
notch = (cq.Workplane("XY").workplane(offset=NOTCH_Z)
         .center(L / 2, 0).rect(4 * T, NOTCH_W).extrude(H)
         .edges("<Z and |X").fillet(NOTCH_R))
body = body.cut(notch)

# ---------------- belt clip ----------------
zt = -CLIP_GAP
zb = -CLIP_DEPTH
ramp_a = CLIP_Y_FLAT - CLIP_Y_FRONT
# side profile (Y, Z): elliptic ramp from the box bottom, tongue with a detent
# bump and a rounded-down tip; extruded across the full attachment width
clip_prof = (cq.Workplane("YZ", origin=(-CLIP_HW_TOP - 1, 0, 0))
             .moveTo(CLIP_Y_FRONT, 0.3)
             .lineTo(CLIP_Y_FRONT, 0.0)
             .ellipseArc(ramp_a, CLIP_DEPTH, 180, 270, startAtCurrent=True)
             .lineTo(CLIP_Y_TIP - 0.4, zb)
             .threePointArc((CLIP_Y_TIP + 0.15, zb + 0.25), (CLIP_Y_TIP - 0.1, zb + 0.6))
             .threePointArc((28.5, -2.43), (CLIP_Y_SLOPE, zt))
             .lineTo(BUMP_Y1, zt)
             .threePointArc(((BUMP_Y0 + BUMP_Y1) / 2, zt + BUMP_H), (BUMP_Y0, zt))
             .lineTo(CLIP_Y_BACKFACE, zt)
             .lineTo(CLIP_Y_BACKFACE, 0.3)
             .close()
             .extrude(2 * CLIP_HW_TOP + 2))
# plan outline: tongue width, flaring out with elliptic arcs to the attachment
flare_x = CLIP_HW_TOP - CLIP_HW
flare_y = CLIP_Y_BACKFACE - CLIP_Y_FRONT
plan = block(-CLIP_HW, CLIP_HW, CLIP_Y_FRONT - 1, CLIP_Y_TIP + 1, -CLIP_DEPTH - 1, 1)
for sx in (-1, 1):
    plan = plan.union(cq.Workplane("XY").workplane(offset=-CLIP_DEPTH - 1)
                      .center(sx * CLIP_HW, CLIP_Y_FRONT)
                      .ellipse(flare_x, flare_y).extrude(CLIP_DEPTH + 2))
# cross-section (XZ) with the lower corners of the flares rounded off
xz = (cq.Workplane("XZ", origin=(0, CLIP_Y_TIP + 2, 0))
      .moveTo(-CLIP_HW_TOP, 0.5)
      .lineTo(-CLIP_HW_TOP, -CLIP_CORNER_Z)
      .ellipseArc(flare_x, CLIP_DEPTH - CLIP_CORNER_Z, 180, 270, startAtCurrent=True)
      .lineTo(CLIP_HW, zb)
      .ellipseArc(flare_x, CLIP_DEPTH - CLIP_CORNER_Z, 270, 360, startAtCurrent=True)
      .lineTo(CLIP_HW_TOP, 0.5)
      .close()
      .extrude(CLIP_Y_TIP - CLIP_Y_FRONT + 4))
clip = clip_prof.intersect(plan).intersect(xz)
body = body.union(clip)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
